import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
S = 0.25                      # design grid -> mm
BALL_R = 78 * S               # ball radius (ball centre at origin)
BAND_Z0 = 56.3 * S            # ball / band junction height
BAND_R = math.sqrt(BALL_R**2 - BAND_Z0**2)
CONE_TOP_Z = 118.5 * S        # flat top of the flared neck (= slot floor)
CONE_TOP_R = 28.6 * S         # neck radius at its top
NECK_Z0 = 61.5 * S            # band cylinder top / start of flared neck
NECK_MID = (39.9 * S, 89.0 * S)  # point on the concave neck flank
NECK_FILLET = 6 * S           # band -> neck blend
SEAM_ANGLE = 180              # deg, where the revolve seam sits

TAB_T = 31.8 * S              # half thickness of fork tab (Y)
TAB_Y_OFF = -0.8 * S          # tab sits very slightly off the ball axis (Y)
TAB_TOP_Z = 159.5 * S         # apex of the rounded tab top
TAB_TOP_HW = 19.3 * S         # half width where the top arc ends
TAB_TAPER = 0.20              # half-width growth per unit depth
TAB_BASE_Z = 60.0 * S         # tab starts inside the neck
TAB_EDGE_R = 2.0 * S          # tiny round on the tab corner edges

SLOT_HW = 21.2 * S            # slot half width (Y)
SLOT_Y_OFF = -1.6 * S         # slot centre offset (Y) -> -Y prong a little thinner
SLOT_Z = CONE_TOP_Z           # slot floor at top of neck
SLOT_R = 12.0 * S             # slot floor corner radius
POCKET_HW = 19.3 * S          # central pocket half length (X)
POCKET_Z = 90.0 * S           # pocket floor

JOIN_FILLET = 10 * S          # tab / neck blend

# ---------------- ball + band + flared neck (revolved) ----------------
# neck side is a shallow concave (trumpet) arc from the band up to the neck top
neck = (cq.Workplane("XZ")
        .moveTo(0, 0)
        .lineTo(BAND_R, 0)
        .lineTo(BAND_R, NECK_Z0)
        .threePointArc(NECK_MID, (CONE_TOP_R, CONE_TOP_Z))
        .lineTo(0, CONE_TOP_Z)
        .close()
        .revolve(360, (0, 0, 0), (0, 1, 0)))
# round the band / neck corner
_band_edge = [e for e in neck.edges().vals()
              if e.geomType() == "CIRCLE" and abs(e.Center().z - NECK_Z0) < 1e-6]
try:
    neck = neck.newObject(_band_edge).fillet(NECK_FILLET)
except Exception:
    pass

ball = cq.Workplane("XY").sphere(BALL_R)
body = ball.union(neck)
# turn the body of revolution so its seam sits at the back-left
body = body.rotate((0, 0, 0), (0, 0, 1), SEAM_ANGLE)

# ---------------- tapered fork tab with rounded top ----------------
alpha = math.atan(TAB_TAPER)                 # side angle from vertical
r_top = TAB_TOP_HW / math.cos(alpha)
cz = TAB_TOP_Z - r_top
tz = cz + r_top * math.sin(alpha)            # tangent point height
bx = TAB_TOP_HW + TAB_TAPER * (tz - TAB_BASE_Z)

tab = (cq.Workplane("XZ")
       .moveTo(-bx, TAB_BASE_Z)
       .lineTo(bx, TAB_BASE_Z)
       .lineTo(TAB_TOP_HW, tz)
       .threePointArc((0, TAB_TOP_Z), (-TAB_TOP_HW, tz))
       .close()
       .extrude(TAB_T, both=True))
# soften the four long corner edges very slightly (lets the blend run round them)
corner_edges = [e for e in tab.edges().vals()
                if e.geomType() == "LINE"
                and abs(abs(e.Center().y) - TAB_T) < 1e-6
                and abs(e.Center().x) > 1e-6]
try:
    tab = tab.newObject(corner_edges).fillet(TAB_EDGE_R)
except Exception:
    pass
tab = tab.translate((0, TAB_Y_OFF, 0))

body = body.union(tab)

# ---------------- blend between tab and neck ----------------
def _is_junction(e):
    c = e.Center()
    return (TAB_BASE_Z + 1 < c.z < CONE_TOP_Z - 0.05
            and math.hypot(c.x, c.y) > TAB_TOP_HW
            and e.geomType() not in ("CIRCLE", "LINE"))

junction = [e for e in body.edges().vals() if _is_junction(e)]
for _r in (JOIN_FILLET, 8 * S, 6 * S):
    try:
        _b = body.newObject(junction).fillet(_r)
        if _b.val().isValid():
            body = _b
            break
    except Exception:
        pass

# ---------------- slot between the prongs (U profile, through) ----------------
_c45 = math.cos(math.radians(45))
slot = (cq.Workplane("YZ")
        .moveTo(-SLOT_HW, SLOT_Z + 100)
        .lineTo(-SLOT_HW, SLOT_Z + SLOT_R)
        .threePointArc((-SLOT_HW + SLOT_R * (1 - _c45), SLOT_Z + SLOT_R * (1 - _c45)),
                       (-SLOT_HW + SLOT_R, SLOT_Z))
        .lineTo(SLOT_HW - SLOT_R, SLOT_Z)
        .threePointArc((SLOT_HW - SLOT_R * (1 - _c45), SLOT_Z + SLOT_R * (1 - _c45)),
                       (SLOT_HW, SLOT_Z + SLOT_R))
        .lineTo(SLOT_HW, SLOT_Z + 100)
        .close()
        .extrude(60, both=True)
        .translate((0, SLOT_Y_OFF, 0)))
body = body.cut(slot)

# ---------------- central pocket between the prongs ----------------
pocket = (cq.Workplane("XY").workplane(offset=POCKET_Z)
          .center(0, SLOT_Y_OFF)
          .rect(2 * POCKET_HW, 2 * SLOT_HW).extrude(100))
body = body.cut(pocket)

result = body
VIEW = {"azimuth": 45, "elevation": 26}
